import math
import cadquery as cq

# ---------------------------------------------------------------
# Bracket: tall back plate (YZ plane), short front wall with round
# side cut-outs, connecting base bars / tabs, rear foot flange.
# X: from back plate (-X) toward front wall (+X); Y: width; Z: up.
# ---------------------------------------------------------------

# ---- global levels -------------------------------------------
FOOT_H = 1.55          # feet protrude below the base bottom
BASE_Z0 = FOOT_H       # bottom of plates / base (feet reach z = 0)
BASE_Z1 = 8.55         # top of base bars / tabs

# ---- tall back plate -------------------------------------------
PL_T = 11.65           # thickness (X)
PL_H = 118.8           # top height
PL_HW = 47.45          # half width (Y)
PL_ARC_Z0 = 12.8       # lower end of concave side arc
PL_ARC_Z1 = 107.1      # upper end of concave side arc
PL_ARC_MIN = 38.2      # half width at the waist
NOTCH_HW = 15.8        # top notch half width
NOTCH_D = 15.85        # top notch depth
PL_HOLE_Y = 20.15      # small face holes near top
PL_HOLE_Z = 110.0
PL_HOLE_D = 4.0
TOP_HOLE_Y = 41.75     # counterbored holes in top faces
TOP_CB_D = 8.0
TOP_CB_DEPTH = 4.0
TOP_HOLE_D = 6.0
TOP_HOLE_DEPTH = 12.0
BK_POCKET_HW = 11.75   # shallow pocket on the back (-X) face
BK_POCKET_Z0 = 17.3
BK_POCKET_Z1 = 100.3
BK_POCKET_DEPTH = 0.8
CSK_Z = 59.55          # countersunk centre hole
CSK_D = 11.5
CSK_HOLE_D = 4.2
TUN_HW = 10.5          # arched opening through plate bottom
TUN_TOP = 14.1         # crown of the arch
TUN_FLOOR = 10.0       # floor of the through part (flush with flange top)
TUN_RECESS = 3.0       # full-height recess depth on the front (+X) face
BOT_HOLE_Y = 18.4
BOT_HOLE_D = 8.0
BOT_HOLE_DEPTH = 10.0

# ---- rear flange ---------------------------------------------------
FL_X0 = -26.75
FL_HW = 23.0
FL_Z1 = 10.0
FL_SLOT_HW = 6.5
FL_SLOT_FLARE = 2.0
FL_SLOT_H = 4.0
FL_SLOT_X0 = -18.0
FL_FILLET = 2.5

# ---- front wall ----------------------------------------------------
FW_X0 = 41.5
FW_T = 11.5
FW_H = 61.9
FW_HW = PL_HW
NOTCH_CY = 52.35       # side cut-out circle centre (|Y|)
NOTCH_CZ = 30.8
NOTCH_R = 19.15
RIB_Y0 = 14.3
RIB_Y1 = 21.6
RIB_Z0 = 45.05
RIB_T = 1.75
POCK_HW = 14.3
POCK_Z0 = 33.3
POCK_D = 1.5
FW_HOLE_Y = 6.8
FW_HOLE_Z = 51.0
FW_HOLE_D = 3.0
NOTCH_FIL_TOP = 4.0
NOTCH_FIL_BOT = 4.0

# ---- base -----------------------------------------------------------
BASE_X1 = 43.25
BAR_Y0 = 36.25         # inner edge of base bars (opening half width)
TAB_X0 = 0.75
TAB_Y1 = 61.75
TAB_HOLE_X = (15.25, 28.95)
TAB_HOLE_Y = 51.05
TAB_HOLE_D = 3.0
FOOT_W = 7.0
FOOT_Y0 = 45.0
TAB_FIL_IN = 1.5
TAB_FIL_OUT = 2.5

# ---- blocks on base --------------------------------------------------
BLK_X0 = 21.75
BLK_X1 = 33.5
BLK_Y0 = BAR_Y0
BLK_Y1 = 47.3
BLK_Z1 = 23.2
BLK_HOLE_D = 8.25
BLK_HOLE_DEPTH = 6.0
BLK_HOLE_Z = 17.6
WEB_Z1 = 10.1
WEB_FILLET = 3.0


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


# ================= profile helper =====================================
# Side contours are built as ONE rational quadratic B-spline edge made of
# exact straight and circular pieces (joined end to end), so that each
# contour gives a single smooth side face.
from OCP.Geom import Geom_BSplineCurve
from OCP.TColgp import TColgp_Array1OfPnt
from OCP.TColStd import TColStd_Array1OfReal, TColStd_Array1OfInteger
from OCP.gp import gp_Pnt
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge


def _arc_ctrl(p, q, c):
    """Middle pole + weight of a rational quadratic circular arc p->q
    (centre c, arc < 180 deg)."""
    vx, vy = p[0] - c[0], p[1] - c[1]
    wx, wy = q[0] - c[0], q[1] - c[1]
    rad = math.hypot(vx, vy)
    half = 0.5 * math.acos(max(-1.0, min(1.0, (vx * wx + vy * wy) / (rad * rad))))
    bx, by = vx + wx, vy + wy
    bl = math.hypot(bx, by)
    d = rad / math.cos(half)
    return (c[0] + bx / bl * d, c[1] + by / bl * d), math.cos(half)


def contour_edge(x, segs):
    """segs: list of ('L', p, q) or ('A', p, q, centre) in (Y, Z) at plane X=x."""
    pts, wts = [segs[0][1]], [1.0]
    for sg in segs:
        p, q = sg[1], sg[2]
        if sg[0] == 'L':
            m, w = ((p[0] + q[0]) / 2.0, (p[1] + q[1]) / 2.0), 1.0
        else:
            m, w = _arc_ctrl(p, q, sg[3])
        pts += [m, q]
        wts += [w, 1.0]
    n = len(segs)
    poles = TColgp_Array1OfPnt(1, len(pts))
    weights = TColStd_Array1OfReal(1, len(pts))
    for i, ((yy, zz), ww) in enumerate(zip(pts, wts)):
        poles.SetValue(i + 1, gp_Pnt(x, yy, zz))
        weights.SetValue(i + 1, ww)
    knots = TColStd_Array1OfReal(1, n + 1)
    mults = TColStd_Array1OfInteger(1, n + 1)
    for i in range(n + 1):
        knots.SetValue(i + 1, float(i))
        mults.SetValue(i + 1, 3 if i in (0, n) else 2)
    curve = Geom_BSplineCurve(poles, weights, knots, mults, 2)
    return cq.Edge(BRepBuilderAPI_MakeEdge(curve).Edge())


def mirror_segs(segs):
    """Mirror a +Y side contour to -Y and reverse its direction."""
    out = []
    for sg in reversed(segs):
        p, q = sg[1], sg[2]
        mp, mq = (-q[0], q[1]), (-p[0], p[1])
        if sg[0] == 'L':
            out.append(('L', mp, mq))
        else:
            out.append(('A', mp, mq, (-sg[3][0], sg[3][1])))
    return out


def profile_solid(x0, thick, bottom_z, top_pts, side_segs):
    """Closed YZ profile: bottom line, +Y side contour (bottom->top), top
    polyline (+Y -> -Y), mirrored -Y side contour; extruded along +X."""
    P = lambda y, z: cq.Vector(x0, y, z)
    yw = side_segs[0][1][0]
    edges = [cq.Edge.makeLine(P(-yw, bottom_z), P(yw, bottom_z)),
             contour_edge(x0, side_segs)]
    for a, b in zip(top_pts[:-1], top_pts[1:]):
        edges.append(cq.Edge.makeLine(P(*a), P(*b)))
    edges.append(contour_edge(x0, mirror_segs(side_segs)))
    face = cq.Face.makeFromWires(cq.Wire.assembleEdges(edges))
    return cq.Solid.extrudeLinear(face, cq.Vector(thick, 0, 0))


# ================= tall plate =======================================
def plate_solid():
    za, zb = PL_ARC_Z0, PL_ARC_Z1
    c = 0.5 * (zb - za)
    sag = PL_HW - PL_ARC_MIN
    r = (c * c + sag * sag) / (2.0 * sag)
    centre = (PL_ARC_MIN + r, 0.5 * (za + zb))
    side = [('L', (PL_HW, BASE_Z0), (PL_HW, za)),
            ('A', (PL_HW, za), (PL_HW, zb), centre),
            ('L', (PL_HW, zb), (PL_HW, PL_H))]
    zn = PL_H - NOTCH_D
    top = [(PL_HW, PL_H), (NOTCH_HW, PL_H), (NOTCH_HW, zn), (-NOTCH_HW, zn),
           (-NOTCH_HW, PL_H), (-PL_HW, PL_H)]
    return profile_solid(-PL_T, PL_T, BASE_Z0, top, side)


plate = cq.Workplane("XY").add(plate_solid())

# rear flange
flange = box(FL_X0, -PL_T + 0.01, -FL_HW, FL_HW, BASE_Z0, FL_Z1)
plate = plate.union(flange)
for s_ in (1, -1):
    plate = plate.edges(cq.selectors.BoxSelector(
        (-PL_T - 0.2, s_ * FL_HW - 0.2, BASE_Z0 + 0.5),
        (-PL_T + 0.2, s_ * FL_HW + 0.2, FL_Z1 - 0.5))).fillet(FL_FILLET)

# ================= front wall =======================================
def wall_solid():
    yw, yc, zc, R = FW_HW, NOTCH_CY, NOTCH_CZ, NOTCH_R
    rt, rb = NOTCH_FIL_TOP, NOTCH_FIL_BOT
    ct = (yw - rt, zc + math.sqrt((R + rt) ** 2 - (yc - yw + rt) ** 2))
    cb = (yw - rb, zc - math.sqrt((R + rb) ** 2 - (yc - yw + rb) ** 2))

    def touch(cf, rf):   # tangent point of fillet circle and notch circle
        dx, dy = cf[0] - yc, cf[1] - zc
        dl = math.hypot(dx, dy)
        return (yc + dx / dl * R, zc + dy / dl * R)

    t2, t3 = touch(cb, rb), touch(ct, rt)
    mid = (yc - R, zc)
    side = [('L', (yw, BASE_Z0), (yw, cb[1])),
            ('A', (yw, cb[1]), t2, cb),
            ('A', t2, mid, (yc, zc)),
            ('A', mid, t3, (yc, zc)),
            ('A', t3, (yw, ct[1]), ct),
            ('L', (yw, ct[1]), (yw, FW_H))]
    top = [(yw, FW_H), (-yw, FW_H)]
    return profile_solid(FW_X0, FW_T, BASE_Z0, top, side)


wall = cq.Workplane("XY").add(wall_solid())

# ribs on the outer face (chamfered bottoms)
for s in (1, -1):
    rib = (
        cq.Workplane("XZ", origin=(0, 0, 0))
        .moveTo(FW_X0 + FW_T - 0.01, RIB_Z0)
        .lineTo(FW_X0 + FW_T + RIB_T, RIB_Z0 + RIB_T)
        .lineTo(FW_X0 + FW_T + RIB_T, FW_H)
        .lineTo(FW_X0 + FW_T - 0.01, FW_H)
        .close()
        .extrude(-(RIB_Y1 - RIB_Y0))
        .translate((0, RIB_Y0 if s > 0 else -RIB_Y1, 0))
    )
    wall = wall.union(rib)

# central pocket with sloped floor
pock = (
    cq.Workplane("XZ")
    .moveTo(FW_X0 + FW_T - POCK_D, POCK_Z0 + POCK_D)
    .lineTo(FW_X0 + FW_T + 0.01, POCK_Z0)
    .lineTo(FW_X0 + FW_T + RIB_T + 1, POCK_Z0)
    .lineTo(FW_X0 + FW_T + RIB_T + 1, FW_H + 1)
    .lineTo(FW_X0 + FW_T - POCK_D, FW_H + 1)
    .close()
    .extrude(-2 * POCK_HW)
    .translate((0, -POCK_HW, 0))
)
wall = wall.cut(pock)

# ================= base bars, tabs, blocks ============================
base = None
for s in (1, -1):
    def ys(a, b):
        return (min(s * a, s * b), max(s * a, s * b))

    y0, y1 = ys(BAR_Y0, PL_HW)
    bar = box(0, BASE_X1, y0, y1, BASE_Z0, BASE_Z1)
    y0, y1 = ys(PL_HW - 0.01, TAB_Y1)
    tab = box(TAB_X0, BASE_X1, y0, y1, BASE_Z0, BASE_Z1)
    # feet under the tab ends, inner ends chamfered at 45 deg
    fz = BASE_Z0 + 0.01
    foot_prof = [(s * FOOT_Y0, fz), (s * (FOOT_Y0 + FOOT_H), 0),
                 (s * TAB_Y1, 0), (s * TAB_Y1, fz)]
    f1 = (cq.Workplane("YZ", origin=(TAB_X0, 0, 0)).polyline(foot_prof)
          .close().extrude(FOOT_W))
    f2 = (cq.Workplane("YZ", origin=(BASE_X1 - FOOT_W, 0, 0)).polyline(foot_prof)
          .close().extrude(FOOT_W))
    y0, y1 = ys(BLK_Y0, BLK_Y1)
    blk = box(BLK_X0, BLK_X1, y0, y1, BASE_Z1 - 0.01, BLK_Z1)
    web = box(BLK_X1 - 0.01, FW_X0 + 0.01, y0, y1, BASE_Z1 - 0.01, WEB_Z1)
    bw = blk.union(web)
    ym = 0.5 * (y0 + y1)
    bw = bw.edges(cq.selectors.BoxSelector(
        (BLK_X1 - 0.3, ym - 3, WEB_Z1 - 0.3), (BLK_X1 + 0.3, ym + 3, WEB_Z1 + 0.3))
    ).fillet(WEB_FILLET)
    part = bar.union(tab).union(f1).union(f2).union(bw)
    base = part if base is None else base.union(part)

result = plate.union(wall).union(base)

# small vertical fillets where the tabs meet the plate and wall end faces
def corner_fill(xc, yc, dx, dy, r, z0, z1):
    """Concave fillet material in the corner at (xc, yc); dx/dy = +-1 give
    the quadrant (into the open space) the fillet occupies."""
    bx = box(min(xc, xc + dx * r), max(xc, xc + dx * r),
             min(yc, yc + dy * r), max(yc, yc + dy * r), z0, z1)
    cyl = (cq.Workplane("XY", origin=(xc + dx * r, yc + dy * r, z0 - 1))
           .circle(r).extrude(z1 - z0 + 2))
    return bx.cut(cyl)


for s_ in (1, -1):
    result = result.union(corner_fill(TAB_X0, s_ * PL_HW, -1, s_, TAB_FIL_IN,
                                      BASE_Z0, BASE_Z1))
    result = result.union(corner_fill(BASE_X1, s_ * PL_HW, 1, s_, TAB_FIL_OUT,
                                      BASE_Z0, BASE_Z1))

# ================= holes / cuts ======================================
# counterbored holes in the top faces of plate and wall
for xc, ztop in ((-PL_T / 2, PL_H), (FW_X0 + FW_T / 2, FW_H)):
    for s in (1, -1):
        cb = (cq.Workplane("XY", origin=(xc, s * TOP_HOLE_Y, ztop - TOP_CB_DEPTH))
              .circle(TOP_CB_D / 2).extrude(TOP_CB_DEPTH + 1))
        th = (cq.Workplane("XY", origin=(xc, s * TOP_HOLE_Y, ztop - TOP_HOLE_DEPTH))
              .circle(TOP_HOLE_D / 2).extrude(TOP_HOLE_DEPTH))
        result = result.cut(cb).cut(th)

# small through holes near the top of the plate
for s in (1, -1):
    h = (cq.Workplane("YZ", origin=(-PL_T - 1, s * PL_HOLE_Y, PL_HOLE_Z))
         .circle(PL_HOLE_D / 2).extrude(PL_T + 2))
    result = result.cut(h)

# shallow pocket on the back face of the plate
bp = box(-PL_T - 1, -PL_T + BK_POCKET_DEPTH, -BK_POCKET_HW, BK_POCKET_HW,
         BK_POCKET_Z0, BK_POCKET_Z1)
result = result.cut(bp)

# countersunk centre hole (countersink on the back side)
csk_depth = (CSK_D - CSK_HOLE_D) / 2.0
bottom_x = -PL_T + BK_POCKET_DEPTH
csk = cq.Solid.makeCone(CSK_D / 2, CSK_HOLE_D / 2, csk_depth,
                        cq.Vector(bottom_x - 0.001, 0, CSK_Z), cq.Vector(1, 0, 0))
result = result.cut(cq.Workplane().add(csk))
ch = (cq.Workplane("YZ", origin=(-PL_T - 1, 0, CSK_Z))
      .circle(CSK_HOLE_D / 2).extrude(PL_T + 2))
result = result.cut(ch)

# arched opening through the bottom of the plate: the arch (segment of a
# circle between the two vertical sides) passes right through above the
# flange-top level; on the front face the full-height arch is recessed.


def arch_prism(x0, x1, z0):
    wp = cq.Workplane("YZ", origin=(x0, 0, 0))
    if z0 < TUN_FLOOR - 1e-6:
        wp = (wp.moveTo(-TUN_HW, z0).lineTo(TUN_HW, z0)
              .lineTo(TUN_HW, TUN_FLOOR))
    else:
        wp = wp.moveTo(TUN_HW, TUN_FLOOR)
    prof = wp.threePointArc((0, TUN_TOP), (-TUN_HW, TUN_FLOOR)).close()
    return prof.extrude(x1 - x0)


result = result.cut(arch_prism(-PL_T - 0.5, 0.5, TUN_FLOOR))
result = result.cut(arch_prism(-TUN_RECESS, 0.5, BASE_Z0 - 1))

# slot under the plate / flange
slot = (cq.Workplane("YZ", origin=(FL_SLOT_X0, 0, 0))
        .polyline([(-FL_SLOT_HW - FL_SLOT_FLARE, BASE_Z0 - 1),
                   (FL_SLOT_HW + FL_SLOT_FLARE, BASE_Z0 - 1),
                   (FL_SLOT_HW + FL_SLOT_FLARE, BASE_Z0),
                   (FL_SLOT_HW, BASE_Z0 + FL_SLOT_H),
                   (-FL_SLOT_HW, BASE_Z0 + FL_SLOT_H),
                   (-FL_SLOT_HW - FL_SLOT_FLARE, BASE_Z0)])
        .close()
        .extrude(0.5 - FL_SLOT_X0))
result = result.cut(slot)

# blind holes in plate bottom
for s in (1, -1):
    h = (cq.Workplane("XY", origin=(-PL_T / 2, s * BOT_HOLE_Y, BASE_Z0 - 1))
         .circle(BOT_HOLE_D / 2).extrude(BOT_HOLE_DEPTH + 1))
    result = result.cut(h)

# holes through the front wall pocket
for s in (1, -1):
    h = (cq.Workplane("YZ", origin=(FW_X0 - 1, s * FW_HOLE_Y, FW_HOLE_Z))
         .circle(FW_HOLE_D / 2).extrude(FW_T + 4))
    result = result.cut(h)

# holes in the tabs
for s in (1, -1):
    for hx in TAB_HOLE_X:
        h = (cq.Workplane("XY", origin=(hx, s * TAB_HOLE_Y, -1))
             .circle(TAB_HOLE_D / 2).extrude(BASE_Z1 + 2))
        result = result.cut(h)

# blind holes in inner faces of the blocks
for s in (1, -1):
    yc = s * 0.5 * (BLK_Y0 + BLK_Y1)
    zc = BLK_HOLE_Z
    h = (cq.Workplane("YZ", origin=(BLK_X0 - 1, yc, zc))
         .circle(BLK_HOLE_D / 2).extrude(BLK_HOLE_DEPTH + 1))
    result = result.cut(h)

VIEW = {"azimuth": 45, "elevation": 26}
